import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 60.0          # outer width  (X) at the base
D = 68.8          # outer depth  (Y) at the base
H = 14.0          # overall height
T_PLATE = 3.0     # top plate thickness
SLOPE_IN = 2.6    # horizontal inset of the sloped upper wall band
Z_SLOPE = 5.3     # height where the vertical base band turns into the slope
WALL_T = 2.4      # skirt wall thickness
C_TOP = 2.5       # corner chamfer leg on sloped band / top face
C_BOT = 1.3       # corner chamfer leg on the vertical base band

# hole pattern (square, offset from the body centre)
HOLE_CX = -3.13
HOLE_CY = -3.9
HOLE_PITCH = 43.25
HOLE_D = 4.4
CBORE_D = 8.2
CBORE_DEPTH = 4.6     # deep counterbore on the +X holes
SLOT_DEPTH = 3.5      # U-slot (open to the -X edge) on the -X holes
SLOT_W = 7.0
BOSS_D = 8.6          # lower boss diameter
BOSS_UP_D = 10.6      # upper (collar) boss diameter around the counterbore
BOSS_STEP_Z = 6.5     # height of the step between collar and lower boss
BOSS_BOTTOM = 0.4

# logo pocket (circle + 90 deg tip toward +X)
POCKET_R = 16.6
POCKET_DEPTH = 0.5
ARCS = [(3.8, 6.9), (7.8, 11.15), (12.0, 15.4)]
WEDGE_R = 2.7

VIEW = {"azimuth": 45, "elevation": 26}

HX0 = HOLE_CX - HOLE_PITCH / 2.0
HX1 = HOLE_CX + HOLE_PITCH / 2.0
HY0 = HOLE_CY - HOLE_PITCH / 2.0
HY1 = HOLE_CY + HOLE_PITCH / 2.0
HOLES = [(HX0, HY0), (HX0, HY1), (HX1, HY0), (HX1, HY1)]


def chamfer_rect(w, d, c):
    hw, hd = w / 2.0, d / 2.0
    return [
        (-hw + c, -hd), (hw - c, -hd), (hw, -hd + c), (hw, hd - c),
        (hw - c, hd), (-hw + c, hd), (-hw, hd - c), (-hw, -hd + c),
    ]


def frustum(w0, d0, w1, d1, c, z0, z1):
    """Ruled loft between two chamfered rectangles (constant chamfer leg)."""
    p0 = chamfer_rect(w0, d0, c)
    p1 = chamfer_rect(w1, d1, c)
    wp = (cq.Workplane("XY").workplane(offset=z0).polyline(p0).close()
          .workplane(offset=z1 - z0).polyline(p1).close())
    return wp.loft(ruled=True)


def prism(w, d, c, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .polyline(chamfer_rect(w, d, c)).close().extrude(z1 - z0))


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# slope rate (horizontal per vertical)
K = SLOPE_IN / (H - Z_SLOPE)
ext = K * Z_SLOPE  # outward growth of the slope extended to z = 0
ZC = H - T_PLATE   # underside of the top plate
HW, HD = W / 2.0, D / 2.0
BIG = 10.0         # generous overcut through the wall thickness

# ---------------- outer body ----------------
outer_f = frustum(W + 2 * ext, D + 2 * ext, W - 2 * SLOPE_IN, D - 2 * SLOPE_IN,
                  C_TOP, 0.0, H)
outer_p = prism(W, D, C_BOT, 0.0, H)
body = outer_f.intersect(outer_p)

# ---------------- inner cavity ----------------
inner_f = frustum(W + 2 * ext - 2 * WALL_T, D + 2 * ext - 2 * WALL_T,
                  W - 2 * SLOPE_IN - 2 * WALL_T, D - 2 * SLOPE_IN - 2 * WALL_T,
                  C_TOP, 0.0, H)
inner_p = prism(W - 2 * WALL_T, D - 2 * WALL_T, C_BOT, -1.0, ZC)
cavity = inner_f.intersect(inner_p)
body = body.cut(cavity)

# ---------------- wall openings ----------------
cuts = []
# front wall (-Y)
cuts.append(box(-20.8, -6.8, -HD - BIG, -HD + BIG, -1, 7.0))
cuts.append(box(-5.0, 10.2, -HD - BIG, -HD + BIG, -1, ZC))
# right wall (+X)
cuts.append(box(HW - BIG, HW + BIG, -19.5, -9.2, -1, ZC))
cuts.append(box(HW - BIG, HW + BIG, -7.3, 2.7, -1, 5.2))
cuts.append(box(HW - BIG, HW + BIG, 15.8, 22.4, -1, 4.5))
cuts.append(box(HW - BIG, HW + BIG, 23.0, 25.8, -1, 2.3))
cuts.append(box(HW - BIG, HW + BIG, 26.4, HD - WALL_T, -1, 4.5))
# right wall latch window (vertical sides, chamfered top corners)
latch = (cq.Workplane("YZ").workplane(offset=HW - BIG)
         .polyline([(5.0, -1.0), (5.0, 1.56), (6.67, 3.15), (10.26, 3.15),
                    (12.0, 1.56), (12.0, -1.0)]).close().extrude(2 * BIG))
cuts.append(latch)
# back wall (+Y): only a segment near the +X corner remains
cuts.append(box(-HW - BIG, 14.2, HD - BIG, HD + BIG, -1, ZC))
cuts.append(box(14.2, 23.8, HD - BIG, HD + BIG, -1, 5.0))
# left wall (-X)
cuts.append(box(-HW - BIG, -HW + BIG, 24.7, HD + BIG, -1, ZC))
cuts.append(box(-HW - BIG, -HW + BIG, -1.6, 14.4, -1, 5.0))
cuts.append(box(-HW - BIG, -HW + BIG, -19.3, -3.8, -1, 7.0))

for c in cuts:
    body = body.cut(c)

# small snap clip inside the latch window
hook = (cq.Workplane("YZ").workplane(offset=HW - WALL_T)
        .polyline([(9.0, 3.3), (10.6, 3.3), (10.6, 0.4), (9.0, 2.0)]).close()
        .extrude(WALL_T - 0.9))
clip = box(HW - 1.7, HW - 0.2, 7.1, 7.9, 0.4, 3.3).union(hook)
body = body.union(clip.intersect(outer_p))

# ---------------- bosses under the screw holes ----------------
for (hx, hy) in HOLES:
    boss = (cq.Workplane("XY").workplane(offset=BOSS_BOTTOM)
            .center(hx, hy).circle(BOSS_D / 2.0).extrude(ZC - BOSS_BOTTOM + 0.5))
    collar = (cq.Workplane("XY").workplane(offset=BOSS_STEP_Z)
              .center(hx, hy).circle(BOSS_UP_D / 2.0).extrude(ZC - BOSS_STEP_Z + 0.5))
    body = body.union(boss.union(collar).intersect(outer_f).intersect(outer_p))


# ---------------- screw holes / counterbores ----------------
for (hx, hy) in HOLES:
    body = body.cut(cq.Workplane("XY").workplane(offset=-1).center(hx, hy)
                    .circle(HOLE_D / 2.0).extrude(H + 2))
    if hx > 0:
        body = body.cut(cq.Workplane("XY").workplane(offset=H - CBORE_DEPTH)
                        .center(hx, hy).circle(CBORE_D / 2.0)
                        .extrude(CBORE_DEPTH + 1))
    else:
        # counterbore that runs out through the -X edge as a U-shaped slot
        ucut = (cq.Workplane("XY").workplane(offset=H - SLOT_DEPTH)
                .center(hx, hy).circle(CBORE_D / 2.0).extrude(SLOT_DEPTH + 1)
                .union(box(-HW - 2, hx, hy - SLOT_W / 2.0, hy + SLOT_W / 2.0,
                           H - SLOT_DEPTH, H + 1)))
        body = body.cut(ucut)

# ---------------- logo pocket + WiFi slots ----------------
pcx, pcy = HOLE_CX, HOLE_CY
tip = POCKET_R * math.sqrt(2.0)
tang = POCKET_R / math.sqrt(2.0)
pocket = (cq.Workplane("XY").workplane(offset=H - POCKET_DEPTH).center(pcx, pcy)
          .moveTo(tip, 0).lineTo(tang, tang)
          .threePointArc((-POCKET_R, 0), (tang, -tang)).close()
          .extrude(POCKET_DEPTH + 1))
body = body.cut(pocket)


def sector(r0, r1, a0=-45.0, a1=45.0):
    ca0, sa0 = math.cos(math.radians(a0)), math.sin(math.radians(a0))
    ca1, sa1 = math.cos(math.radians(a1)), math.sin(math.radians(a1))
    wp = cq.Workplane("XY").workplane(offset=ZC - 1).center(pcx, pcy)
    if r0 <= 0:
        wp = (wp.moveTo(0, 0).lineTo(r1 * ca0, r1 * sa0)
              .threePointArc((r1, 0), (r1 * ca1, r1 * sa1)).close())
    else:
        wp = (wp.moveTo(r0 * ca0, r0 * sa0).lineTo(r1 * ca0, r1 * sa0)
              .threePointArc((r1, 0), (r1 * ca1, r1 * sa1))
              .lineTo(r0 * ca1, r0 * sa1)
              .threePointArc((r0, 0), (r0 * ca0, r0 * sa0)).close())
    return wp.extrude(T_PLATE + 2)


body = body.cut(sector(0, WEDGE_R))
for (r0, r1) in ARCS:
    body = body.cut(sector(r0, r1))

result = body
